import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 100.0          # overall height (Z)
W = 45.0           # overall depth (Y)
L_LOOP = 30.8      # length of the closed loop/frame along X
L_TOT = 57.7       # overall length along X (loop + block)
T = 4.0            # loop wall thickness (sides and top)
T_BOT = 3.0        # loop bottom wall thickness

C_TOP = 6.1        # outer chamfer, top corners of loop
C_BOT_F_Y = 4.0    # outer chamfer, bottom -Y edge (full length), Y leg
C_BOT_F_Z = 3.1    #   ... Z leg
C_BOT_B_Y = 7.3    # outer chamfer, bottom +Y edge (loop portion only), Y leg
C_BOT_B_Z = 5.0    #   ... Z leg
C_IN = 4.0         # inner chamfers of the loop opening

H_BLOCK = 33.7     # block top height
X_GROOVE = 37.2    # groove end (x) next to the loop
H_GROOVE = 27.8    # groove floor height
X_PLAT = 24.5      # inner platform start (inside loop, up to groove floor)
SLOT_Y0 = 17.3     # through slot in groove floor
SLOT_Y1 = 30.5
POCKET_Y0 = 9.5    # shallow pocket widening the slot at the top
POCKET_DEPTH = 4.0
Y_STEP = 35.2      # step on the +Y side of the block
H_STEP = 12.75

HOLE_D = 5.0       # holes in the +X face
HOLE_Z = 7.75
HOLE_Y = (14.5, 34.9)
HOLE_DEPTH = 10.0

# wall notch (side profile, XZ): line from (0, N_TOP) tangent to circle
N_TOP = 77.6
N_CX = 2.0
N_CZ = 49.6
N_R = 14.2


def chamfered_rect(y0, z0, y1, z1, c_bl, c_br, c_tr, c_tl):
    """points of a rectangle in (y, z) with corner chamfers.

    each chamfer is (leg_y, leg_z) or a single number for a 45 deg chamfer;
    bl = (-y,-z) corner, br = (+y,-z), tr = (+y,+z), tl = (-y,+z).
    """
    def legs(c):
        if isinstance(c, (tuple, list)):
            return c
        return (c, c)
    bl, br, tr, tl = legs(c_bl), legs(c_br), legs(c_tr), legs(c_tl)
    pts = [
        (y0 + bl[0], z0), (y1 - br[0], z0),
        (y1, z0 + br[1]), (y1, z1 - tr[1]),
        (y1 - tr[0], z1), (y0 + tl[0], z1),
        (y0, z1 - tl[1]), (y0, z0 + bl[1]),
    ]
    out = []
    for p in pts:
        if not out or (abs(p[0] - out[-1][0]) > 1e-9 or abs(p[1] - out[-1][1]) > 1e-9):
            out.append(p)
    if abs(out[0][0] - out[-1][0]) < 1e-9 and abs(out[0][1] - out[-1][1]) < 1e-9:
        out.pop()
    return out


# ---------------- loop (tube along X) ----------------
outer_pts = chamfered_rect(0, 0, W, H, (C_BOT_F_Y, C_BOT_F_Z),
                           (C_BOT_B_Y, C_BOT_B_Z), C_TOP, C_TOP)
inner_pts = chamfered_rect(T, T_BOT, W - T, H - T, C_IN, C_IN, C_IN, C_IN)

# YZ workplane: local x -> Y, local y -> Z, normal -> +X
loop = (
    cq.Workplane("YZ")
    .polyline(outer_pts).close()
    .extrude(L_LOOP)
)
cavity = (
    cq.Workplane("YZ")
    .workplane(offset=-1)
    .polyline(inner_pts).close()
    .extrude(L_LOOP + 2)
)
loop = loop.cut(cavity)

# ---------------- notch in both side walls ----------------
# tangent point of the line from (0, N_TOP) onto the circle
dx, dz = N_CX - 0.0, N_CZ - N_TOP
d = math.hypot(dx, dz)
ang_c = math.atan2(dz, dx)
ang_off = math.asin(N_R / d)
ang_line = ang_c + ang_off          # direction of the tangent line
lt = math.sqrt(d * d - N_R * N_R)
tx, tz = lt * math.cos(ang_line), N_TOP + lt * math.sin(ang_line)
# bottom end of arc on x = 0
bz = N_CZ - math.sqrt(N_R ** 2 - N_CX ** 2)
mid = (N_CX + N_R, N_CZ)            # rightmost point of circle

notch = (
    cq.Workplane("XZ")
    .moveTo(-5, N_TOP)
    .lineTo(0, N_TOP)
    .lineTo(tx, tz)
    .threePointArc(mid, (0, bz))
    .lineTo(-5, bz)
    .close()
    .extrude(-(W + 10))
    .translate((0, -5, 0))
)
loop = loop.cut(notch)

# ---------------- base block ----------------
block = (
    cq.Workplane("YZ")
    .workplane(offset=L_LOOP)
    .polyline(chamfered_rect(0, 0, W, H_BLOCK, (C_BOT_F_Y, C_BOT_F_Z), 0, 0, 0)).close()
    .extrude(L_TOT - L_LOOP)
)
body = loop.union(block)

# platform filling the +X end of the loop cavity up to the groove floor
plat = (
    cq.Workplane("YZ")
    .workplane(offset=X_PLAT)
    .polyline(inner_pts).close()
    .extrude(L_LOOP - X_PLAT + 0.5)
    .intersect(
        cq.Workplane("XY").box(L_TOT, W, H_GROOVE, centered=False)
    )
)
body = body.union(plat)

# groove between loop and block (open to -Y, closed by +Y wall)
groove = cq.Workplane("XY").box(
    X_GROOVE - L_LOOP, W - T + 1, H_BLOCK - H_GROOVE + 1, centered=False
).translate((L_LOOP, -1, H_GROOVE))
body = body.cut(groove)

# rectangular through slot in the groove floor
slot = cq.Workplane("XY").box(
    X_GROOVE - L_LOOP, SLOT_Y1 - SLOT_Y0, H_GROOVE + 2, centered=False
).translate((L_LOOP, SLOT_Y0, -1))
body = body.cut(slot)

pocket = cq.Workplane("XY").box(
    X_GROOVE - L_LOOP, SLOT_Y1 - POCKET_Y0, POCKET_DEPTH + 1, centered=False
).translate((L_LOOP, POCKET_Y0, H_GROOVE - POCKET_DEPTH))
body = body.cut(pocket)

# step on the +Y side of the block
step = cq.Workplane("XY").box(
    L_TOT - X_GROOVE + 1, W - Y_STEP + 1, H_BLOCK, centered=False
).translate((X_GROOVE, Y_STEP, H_STEP))
body = body.cut(step)

# two blind holes in the +X face (seam of the bore placed on the hidden -Y side)
hole_plane = cq.Plane(origin=(L_TOT + 1, 0, 0), xDir=(0, -1, 0), normal=(-1, 0, 0))
holes = (
    cq.Workplane(hole_plane)
    .pushPoints([(-hy, HOLE_Z) for hy in HOLE_Y])
    .circle(HOLE_D / 2)
    .extrude(HOLE_DEPTH + 1)
)
body = body.cut(holes).clean()

# imprint the two face seams seen on the target (coplanar faces kept separate):
#  - groove end wall vs. inner face of the +Y loop wall (plane y = W - T)
#  - +X face of the wall extension vs. ledge face below the groove (plane x = X_GROOVE)
seam_a = cq.Face.makeFromWires(
    cq.Wire.makePolygon(
        [cq.Vector(L_LOOP, W - T, H_GROOVE), cq.Vector(X_GROOVE, W - T, H_GROOVE),
         cq.Vector(X_GROOVE, W - T, H_BLOCK), cq.Vector(L_LOOP, W - T, H_BLOCK)],
        close=True,
    )
)
seam_b = cq.Face.makeFromWires(
    cq.Wire.makePolygon(
        [cq.Vector(X_GROOVE, W - T, H_STEP), cq.Vector(X_GROOVE, W, H_STEP),
         cq.Vector(X_GROOVE, W, H_BLOCK), cq.Vector(X_GROOVE, W - T, H_BLOCK)],
        close=True,
    )
)
solid = body.val()
try:
    split = solid.split(seam_a, seam_b)
    sols = split.Solids()
    if len(sols) == 1 and sols[0].isValid() and abs(sols[0].Volume() - solid.Volume()) < 1e-3:
        solid = sols[0]
except Exception:
    pass

result = cq.Workplane("XY").newObject([solid])

VIEW = {"azimuth": 45, "elevation": 26}
